import cadquery as cq

# camera for the harness render (default view)
VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- driving dimensions (mm) ----------------
L = 100.0      # block length (X)
W = 60.0       # block width  (Y)
H = 40.0       # block height (Z)
CH = 5.0       # vertical corner chamfer

# corner bolt holes (on the +Y side), counterbored from below
HOLE_D = 6.0
HOLE_Y = 21.0                  # hole centre Y
HOLE_XL, HOLE_XR = -41.0, 42.0  # hole centre X (left / right)
CB_DL, CB_DR = 10.0, 11.5      # counterbore diameters (left / right)
CB_DEPTH = 9.0                 # counterbore depth from the underside

# through slot in the top face
SLOT_X0, SLOT_X1 = -6.0, 33.0
SLOT_W = 10.0
SLOT_R = 2.0

# large rectangular pocket in the underside
PK_X0, PK_X1 = -28.2, 32.9
PK_Y0, PK_Y1 = -14.75, 14.05
PK_DEPTH = 10.0
PK_R = 3.0

# lower (longer) slot opening from the pocket ceiling
LS_X0, LS_X1 = -20.0, 33.0
LS_TOP = 15.0          # z of the lower slot ceiling
LS_R = 3.0

# narrow pocket near the -X end of the underside
NP_X0, NP_X1 = -43.0, -35.0
NP_Y0, NP_Y1 = PK_Y0, PK_Y1
NP_DEPTH = 6.5
NP_R = 2.5


def rrect_prism(x0, x1, y0, y1, z0, z1, r):
    """Axis-aligned prism with rounded vertical edges."""
    b = (cq.Workplane("XY").workplane(offset=z0)
         .center((x0 + x1) / 2.0, (y0 + y1) / 2.0)
         .rect(x1 - x0, y1 - y0).extrude(z1 - z0))
    if r > 0:
        b = b.edges("|Z").fillet(r)
    return b


def cyl(x, y, d, z0, z1):
    return (cq.Workplane("XY").workplane(offset=z0).center(x, y)
            .circle(d / 2.0).extrude(z1 - z0))


# main block with chamfered vertical corners
body = (cq.Workplane("XY").rect(L, W).extrude(H)
        .edges("|Z").chamfer(CH))

# bolt holes + counterbores from underside
for hx, cbd in ((HOLE_XL, CB_DL), (HOLE_XR, CB_DR)):
    body = body.cut(cyl(hx, HOLE_Y, HOLE_D, -1, H + 1))
    body = body.cut(cyl(hx, HOLE_Y, cbd, -1, CB_DEPTH))

# top through slot
body = body.cut(rrect_prism(SLOT_X0, SLOT_X1, -SLOT_W / 2, SLOT_W / 2, -1, H + 1, SLOT_R))

# underside pocket
body = body.cut(rrect_prism(PK_X0, PK_X1, PK_Y0, PK_Y1, -1, PK_DEPTH, PK_R))

# lower slot above the pocket ceiling
body = body.cut(rrect_prism(LS_X0, LS_X1, -SLOT_W / 2, SLOT_W / 2, -1, LS_TOP, LS_R))

# narrow pocket at -X end of underside
body = body.cut(rrect_prism(NP_X0, NP_X1, NP_Y0, NP_Y1, -1, NP_DEPTH, NP_R))

result = body
